import math

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 180.0          # overall width (X)
H = 102.0          # overall height (Z)
R_CORNER = 42.0    # plan-view corner radius
T = 3.7            # plate thickness (Y)
EDGE_FILLET = 2.0  # round on the back perimeter edge

HOLE_SPACING = 162.5   # mounting hole pitch (X)
HOLE_D = 6.3           # mounting hole diameter
CSK_D = 12.8           # countersink diameter (at the rim, back side)
CSK_ANGLE = 82.0       # countersink included angle
RIM_BASE_D = 13.8      # low conical rim raised around each countersink
RIM_H = 0.45           # rim height above the back face

SQ = 13.3              # square window size
SQ_Z = 37.6            # square window centre height

SLOT_W = 20.0          # lower slot width
SLOT_H = 8.8           # lower slot height
SLOT_Z = -32.2         # lower slot centre height
SLOT_X = -0.5          # lower slot centre offset
SLOT_CH = 2.0          # chamfer on the two lower slot corners

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- plate body ----------------
# Plate lies in the XZ plane, front face at Y=0, back face at Y=T.
plate = (
    cq.Workplane("XZ")
    .sketch()
    .rect(W, H)
    .vertices()
    .fillet(R_CORNER)
    .finalize()
    .extrude(-T)          # XZ normal is -Y, so a negative extrude goes +Y
)

# rounded perimeter edge on the back face
plate = plate.faces(">Y").edges().fillet(EDGE_FILLET)

hole_xs = [-HOLE_SPACING / 2, HOLE_SPACING / 2]

# low conical rims on the back around the mounting holes
for x in hole_xs:
    rim = cq.Solid.makeCone(
        RIM_BASE_D / 2, CSK_D / 2, RIM_H,
        cq.Vector(x, T - 0.01, 0), cq.Vector(0, 1, 0)
    )
    plate = plate.union(cq.Workplane().add(rim))

# mounting holes, countersunk from the back
top = T - 0.01 + RIM_H
csk_depth = (CSK_D - HOLE_D) / 2.0 / math.tan(math.radians(CSK_ANGLE / 2))
for x in hole_xs:
    hole = cq.Solid.makeCylinder(
        HOLE_D / 2, T + RIM_H + 2, cq.Vector(x, -1, 0), cq.Vector(0, 1, 0)
    )
    cone = cq.Solid.makeCone(
        HOLE_D / 2, CSK_D / 2 + 0.05, csk_depth + 0.05,
        cq.Vector(x, top - csk_depth, 0), cq.Vector(0, 1, 0)
    )
    plate = plate.cut(cq.Workplane().add(hole)).cut(cq.Workplane().add(cone))

# square window (upper)
sq = (
    cq.Workplane("XZ", origin=(0, T + 5, 0))
    .center(0, SQ_Z)
    .rect(SQ, SQ)
    .extrude(T + 10)
)
plate = plate.cut(sq)

# lower slot with chamfered bottom corners
c = SLOT_CH
hw, hh = SLOT_W / 2, SLOT_H / 2
pts = [
    (SLOT_X - hw, SLOT_Z + hh),
    (SLOT_X + hw, SLOT_Z + hh),
    (SLOT_X + hw, SLOT_Z - hh + c),
    (SLOT_X + hw - c, SLOT_Z - hh),
    (SLOT_X - hw + c, SLOT_Z - hh),
    (SLOT_X - hw, SLOT_Z - hh + c),
]
slot = (
    cq.Workplane("XZ", origin=(0, T + 5, 0))
    .polyline(pts)
    .close()
    .extrude(T + 10)
)
plate = plate.cut(slot)

result = plate
